"""Spur gear: 45 teeth, module 2, 20 deg involute, plain disc with centre bore."""
import math
import cadquery as cq

# ---------------- driving dimensions (mm / deg) ----------------
MODULE = 2.0            # gear module
TEETH = 45              # number of teeth
PRESSURE_ANGLE = 20.0   # involute pressure angle
FACE_WIDTH = 15.4       # gear thickness (along Z)
BORE_D = 15.2           # centre bore diameter
ADDENDUM = 1.0 * MODULE
DEDENDUM = 1.25 * MODULE
TIP_ROUND = 0.06 * MODULE     # how far the tip corner sits below the tip circle
ROOT_BLEND = 0.55             # 0..1, how far the root blend reaches into the gap
TIP_CORNER = 0.85            # angular position of tip corner point (fraction of tip half-angle)

# ---------------- derived gear geometry ----------------
rp = MODULE * TEETH / 2.0                               # pitch radius
rb = rp * math.cos(math.radians(PRESSURE_ANGLE))        # base radius
ra = rp + ADDENDUM                                      # tip radius
rf = rp - DEDENDUM                                      # root radius
pitch = 2.0 * math.pi / TEETH                           # angular pitch


def inv(a):
    """involute function"""
    return math.tan(a) - a


# half tooth thickness angle measured at the base circle
half_base = math.pi / (2 * TEETH) + inv(math.radians(PRESSURE_ANGLE))


def flank_angle(r):
    """polar angle of the involute flank at radius r (tooth centred on 0)"""
    rr = max(r, rb)
    return half_base - inv(math.acos(rb / rr))


def polar(r, a):
    return cq.Vector(r * math.cos(a), r * math.sin(a), 0)


# ---- one tooth, from the middle of one root gap to the middle of the next ----
# lower half: root middle -> root blend -> involute flank -> rounded tip corner
a_root = flank_angle(rf)
a_tip = flank_angle(ra)
half = [
    polar(rf, -pitch / 2),                                             # root middle
    polar(rf + 0.05, -(a_root + ROOT_BLEND * (pitch / 2 - a_root))),   # root blend
]
for r in (rf + 0.4 * MODULE, rp - 0.25 * MODULE, rp + 0.2 * MODULE, ra - 0.35 * MODULE):
    half.append(polar(r, -flank_angle(r)))                             # involute flank
half.append(polar(ra - TIP_ROUND, -TIP_CORNER * a_tip))                      # tip corner
tooth_pts = half + [polar(ra, 0.0)] + [cq.Vector(p.x, -p.y, 0) for p in reversed(half)]

# chord-length parameters, unit tangents at the root middles (tangent to root circle)
params = [0.0]
for i in range(1, len(tooth_pts)):
    params.append(params[-1] + (tooth_pts[i] - tooth_pts[i - 1]).Length)
t_start = cq.Vector(math.sin(pitch / 2), math.cos(pitch / 2), 0)
t_end = cq.Vector(-math.sin(pitch / 2), math.cos(pitch / 2), 0)
tooth_edge = cq.Edge.makeSpline(tooth_pts, tangents=[t_start, t_end],
                                scale=False, parameters=params)

# ---- polar pattern of the tooth edge -> closed outline ----
z_axis = cq.Vector(0, 0, 1)
origin = cq.Vector(0, 0, 0)
edges = [tooth_edge.rotate(origin, z_axis, math.degrees(k * pitch)) for k in range(TEETH)]
outline = cq.Wire.assembleEdges(edges)

# ---- extrude the toothed blank and cut the bore ----
blank = cq.Solid.extrudeLinear(cq.Face.makeFromWires(outline), cq.Vector(0, 0, FACE_WIDTH))
gear = (
    cq.Workplane("XY")
    .add(blank)
    .faces(">Z")
    .workplane()
    .hole(BORE_D)
)

# orient so that one tooth points along +Y (as in the reference)
gear = gear.rotate((0, 0, 0), (0, 0, 1), 90)

result = gear

VIEW = {"azimuth": 45, "elevation": 26}
